"""Square cover / cap: rounded block with a pocket open at the bottom,
one hole in the front wall, one larger hole in the left wall and a
zig-zag (checkerboard) row of seven holes in the back wall."""
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 85.0            # outer width  (X)
D = 85.0            # outer depth  (Y)
H = 40.5            # outer height (Z)
R_OUT = 5.0         # outer vertical corner radius
T_WALL = 5.2        # side wall thickness
T_TOP = 5.7         # top (ceiling) thickness
R_IN = 0.0          # inner vertical corner radius of the pocket (sharp)

Z_HOLE = 20.0       # centre height of the hole pattern above the open bottom

D_FRONT = 6.0       # front (-Y) wall: single centred hole
D_LEFT = 7.8        # left  (-X) wall: single centred larger hole
D_BACK = 6.0        # back  (+Y) wall: zig-zag row of holes
PITCH = 10.0        # horizontal pitch = vertical spacing of the two rows
N_BACK = 7          # number of back holes (odd -> symmetric about X=0)

# ---------------- body ----------------
outer = (
    cq.Workplane("XY")
    .rect(W, D)
    .extrude(H)
    .edges("|Z").fillet(R_OUT)
)

pocket = (
    cq.Workplane("XY")
    .rect(W - 2 * T_WALL, D - 2 * T_WALL)
    .extrude(H - T_TOP)
)
if R_IN > 0.0:
    pocket = pocket.edges("|Z").fillet(R_IN)

body = outer.cut(pocket)

# ---------------- holes ----------------
CUT_LEN = T_WALL + 10.0   # cutter length, starts 5 mm outside the wall

# front hole through the -Y wall (XZ plane normal is -Y, so extrude negative -> +Y)
front_cut = (
    cq.Workplane("XZ", origin=(0, -D / 2 - 5.0, 0))
    .center(0, Z_HOLE)
    .circle(D_FRONT / 2.0)
    .extrude(-CUT_LEN)
)

# left hole through the -X wall (YZ plane normal is +X)
left_cut = (
    cq.Workplane("YZ", origin=(-W / 2 - 5.0, 0, 0))
    .center(0, Z_HOLE)
    .circle(D_LEFT / 2.0)
    .extrude(CUT_LEN)
)

# back holes through the +Y wall: x = k*PITCH (k = -3..3);
# even k on the upper row, odd k on the lower row (checkerboard zig-zag)
back_pts = []
half = (N_BACK - 1) // 2
for k in range(-half, half + 1):
    z = Z_HOLE + PITCH / 2.0 if k % 2 == 0 else Z_HOLE - PITCH / 2.0
    back_pts.append((k * PITCH, z))
back_cut = (
    cq.Workplane("XZ", origin=(0, D / 2 + 5.0, 0))
    .pushPoints(back_pts)
    .circle(D_BACK / 2.0)
    .extrude(CUT_LEN)
)

body = body.cut(front_cut).cut(left_cut).cut(back_cut)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
